"""Vertical (top-entry) micro-USB type-B receptacle: folded sheet-metal shell with a
jigsaw seam, flared entry lips, side hold-down tabs, latch springs, bottom posts and
SMT feet, plus the plastic insert (tongue with 5 contacts, front pin block with 5 pins).
X = width, Y = depth (-Y front with seam and pins), Z = up (mating face on top)."""
import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
W = 7.6          # shell outer width  (X)
D = 2.42         # shell outer depth  (Y)
H = 5.10         # shell height       (Z)
T = 0.22         # sheet thickness
CX = 1.00        # -Y corner chamfer, X leg
CY = 1.00        # -Y corner chamfer, Y leg
R_BACK = 0.40    # +Y vertical corner radius
R_CH = 0.50      # bend radius at the chamfer corners

# top flares / ears
FL_R = 0.30      # bend radius of flares
FL_ANG = 60.0    # bend angle (deg from vertical)
FL_L = 0.16      # straight lip after the bend
FLF_HW = 2.65    # half width of -Y (front) flare
FLB_HW = 3.20    # half width of +Y (back) flare
EAR_W = 0.78     # ear width (Y)
EAR_YC = 0.31    # ear centre (Y)
FL_TIP_R = 0.20  # rounded corners of the flare tips
EAR_TIP_R = 0.20

# side windows
WIN_Z0, WIN_Z1 = 2.22, 3.64     # upper side window
WIN_Y1 = 0.30                   # +Y end of upper window
WIN_R = 0.25                    # corner radius of the side windows
LWIN_Z0, LWIN_Z1 = 0.95, 1.54   # lower side window (its bottom = top of the bottom post)
LWIN_Y1 = -0.13
WIN_XIN = 2.80                  # inner X where the corner cut stops
TAB_Y = -1.82                   # tab tip (Y)
TAB_Z0, TAB_Z1 = 2.44, 3.40     # tab height range
TAB_XB = 3.65                   # X of the tab plate mid-plane
TAB_RC = 0.30                   # tab bend radius (mid-plane)
TAB_TIP_R = 0.25                # rounded tab corners

# front (-Y) bottom, plastic block and pins
FRONT_CUT_Z = 1.54
BLK_HW = 1.75
BLK_CH = 0.30
PIN_N = 5
PIN_P = 0.65
PIN_W = 0.27
PIN_H = 0.80
PIN_PROUD = 0.10
FTAB_X0, FTAB_X1, FTAB_Z0 = 1.86, 2.42, 1.21

# feet / bottom posts
FOOT_X0, FOOT_X1 = 2.20, 2.90
POST_X0, POST_Y1 = 2.2, D / 2 - T
POST_R_IN = 0.68   # radius of the inner front vertical edge of the post
FOOT_Y = -1.82
FOOT_RIM = 0.08     # rim width of the folded foot (seen from below)
FOOT_POCKET = 0.10

# back (+Y) latches
LATCH_XC = 2.47
LATCH_W = 1.25
LATCH_Z0, LATCH_Z1 = 2.65, 4.58
LATCH_ANG = 65.0   # outward bend of the latch lip (deg from vertical)
LATCH_L = 0.30
LIP_W = 1.00
SPR_ANG = 25.0     # inner spring lean (deg from vertical)
SPR_L = 0.85
SPR_W = 0.60
BN_X0, BN_X1, BN_Z = 2.12, 3.22, 1.10   # back wall bottom notches
BS_X0, BS_Z = 1.37, 0.60                # step next to them
BM_X, BM_Z = 0.65, 0.50                 # central bottom notch

# insert / tongue
FLOOR_Z = 1.9
TONGUE_HW = 1.80
TONGUE_Y0, TONGUE_Y1 = 0.07, 0.72
CONT_W = 0.34       # contact width
CONT_PROUD = 0.13   # contact protrusion from the tongue face
TONGUE_TOP = H - 0.75
INS_Z0 = 0.25

# seam
SEAM_GAP = 0.044
SEAM_R = 0.15


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(abs(x1 - x0), abs(y1 - y0), abs(z1 - z0), centered=False)
            .translate((min(x0, x1), min(y0, y1), min(z0, z1))))


def rrect(x0, x1, y0, y1, r_ll, r_lr, r_ur, r_ul, z=0.0):
    """closed rounded rectangle wire in the XY plane with a radius per corner
    (lower-left, lower-right, upper-right, upper-left)"""
    c = math.cos(math.radians(45))
    wp = cq.Workplane("XY", origin=(0, 0, z)).moveTo(x0 + r_ll, y0)
    wp = wp.lineTo(x1 - r_lr, y0)
    wp = wp.threePointArc((x1 - r_lr + r_lr * c, y0 + r_lr - r_lr * c), (x1, y0 + r_lr))
    wp = wp.lineTo(x1, y1 - r_ur)
    wp = wp.threePointArc((x1 - r_ur + r_ur * c, y1 - r_ur + r_ur * c), (x1 - r_ur, y1))
    wp = wp.lineTo(x0 + r_ul, y1)
    wp = wp.threePointArc((x0 + r_ul - r_ul * c, y1 - r_ul + r_ul * c), (x0, y1 - r_ul))
    wp = wp.lineTo(x0, y0 + r_ll)
    wp = wp.threePointArc((x0 + r_ll - r_ll * c, y0 + r_ll - r_ll * c), (x0 + r_ll, y0))
    return wp.close()


def near_z_edges(wp, pts, r):
    """fillet vertical edges nearest to each (x, y) point"""
    for (x, y) in pts:
        wp = wp.edges(cq.selectors.NearestToPointSelector((x, y, H / 2))).fillet(r)
    return wp


# ---------------- shell tube ----------------
prof = [(-W / 2, D / 2), (W / 2, D / 2), (W / 2, -D / 2 + CY), (W / 2 - CX, -D / 2),
        (-W / 2 + CX, -D / 2), (-W / 2, -D / 2 + CY)]
outer = cq.Workplane("XY").polyline(prof).close().extrude(H)
outer = near_z_edges(outer, [(W / 2, D / 2), (-W / 2, D / 2)], R_BACK)
outer = near_z_edges(outer, [(W / 2, -D / 2 + CY), (-W / 2, -D / 2 + CY),
                             (W / 2 - CX, -D / 2), (-W / 2 + CX, -D / 2)], R_CH)
shell = outer.faces(">Z or <Z").shell(-T)


# ---------------- flares (bent-out lips) ----------------
def flare_profile_pts(y_out, sgn):
    """2D points (u=horizontal, v=Z) for a lip bent outward from a wall whose outer
    face is at u=y_out and which lies on the inner side (sgn = direction of 'outward')."""
    a = math.radians(FL_ANG)
    c = y_out + sgn * FL_R                     # bend centre (u)
    r_in, r_out = FL_R, FL_R + T
    def arcpt(r, ang):
        return (c - sgn * r * math.cos(ang), H + r * math.sin(ang))
    p0 = (y_out, H)
    p1 = arcpt(r_in, a / 2)
    p2 = arcpt(r_in, a)
    d = (sgn * math.sin(a), math.cos(a))
    p3 = (p2[0] + d[0] * FL_L, p2[1] + d[1] * FL_L)
    q2 = arcpt(r_out, a)
    q3 = (q2[0] + d[0] * FL_L, q2[1] + d[1] * FL_L)
    q1 = arcpt(r_out, a / 2)
    q0 = (y_out - sgn * T, H)
    return p0, p1, p2, p3, q3, q2, q1, q0


def flare_solid(plane, y_out, sgn, half_w):
    p0, p1, p2, p3, q3, q2, q1, q0 = flare_profile_pts(y_out, sgn)
    wp = (cq.Workplane(plane, origin=(0, 0, 0))
          .moveTo(*p0).threePointArc(p1, p2).lineTo(*p3).lineTo(*q3)
          .lineTo(*q2).threePointArc(q1, q0).close())
    return wp.extrude(half_w, both=True)


# front (-Y) and back (+Y) flares: profile in the YZ plane (local x = Y, local y = Z)
fl_front = flare_solid("YZ", -D / 2, -1, FLF_HW)
fl_back = flare_solid("YZ", D / 2, 1, FLB_HW)
# ears on the +-X walls: profile in XZ plane (local x = X, local y = Z), extruded along Y
ear_r = flare_solid("XZ", W / 2, 1, EAR_W / 2).translate((0, EAR_YC, 0))
ear_l = flare_solid("XZ", -W / 2, -1, EAR_W / 2).translate((0, EAR_YC, 0))


def round_tip(wp, d, along, r):
    """round the two outer corners of a lip (edges across the sheet at the tip)"""
    try:
        return (wp.faces(cq.selectors.DirectionMinMaxSelector(d, True))
                .edges("not |" + along).fillet(r))
    except Exception:
        return wp


_sa, _ca = math.sin(math.radians(FL_ANG)), math.cos(math.radians(FL_ANG))
fl_front = round_tip(fl_front, cq.Vector(0, -_sa, _ca), "X", FL_TIP_R)
fl_back = round_tip(fl_back, cq.Vector(0, _sa, _ca), "X", FL_TIP_R)
ear_r = round_tip(ear_r, cq.Vector(_sa, 0, _ca), "Y", EAR_TIP_R)
ear_l = round_tip(ear_l, cq.Vector(-_sa, 0, _ca), "Y", EAR_TIP_R)

shell = shell.union(fl_front).union(fl_back).union(ear_r).union(ear_l)

# ---------------- side windows through the -Y corners ----------------
for s_ in (1, -1):
    xin, xout = s_ * WIN_XIN, s_ * (W / 2 + 0.5)
    # upper window (corner cut)
    wc = box(xin, xout, -D / 2 - 0.5, WIN_Y1, WIN_Z0, WIN_Z1)
    wc = wc.faces(">Y").edges("|X").fillet(WIN_R)
    shell = shell.cut(wc)
    # lower window
    lwc = box(s_ * 2.42, xout, -D / 2 - 0.5, LWIN_Y1, LWIN_Z0, LWIN_Z1)
    lwc = lwc.faces(">Y").edges("|X").fillet(WIN_R)
    shell = shell.cut(lwc)
    # bent tab: flange -> 90 deg bend -> plate pointing -Y (profile in plan, extruded in Z)
    yc = -D / 2 + T / 2                  # flange mid-plane
    xb = TAB_XB - TAB_RC                 # start of the bend
    cyb = yc - TAB_RC                    # bend centre (Y)
    ri, ro = TAB_RC - T / 2, TAB_RC + T / 2
    c45 = math.cos(math.radians(45))
    strap = (cq.Workplane("XY", origin=(0, 0, TAB_Z0))
             .moveTo(s_ * (WIN_XIN - 0.1), yc + T / 2)
             .lineTo(s_ * xb, yc + T / 2)
             .threePointArc((s_ * (xb + ro * c45), cyb + ro * c45), (s_ * (xb + ro), cyb))
             .lineTo(s_ * (xb + ro), TAB_Y)
             .lineTo(s_ * (xb + ri), TAB_Y)
             .lineTo(s_ * (xb + ri), cyb)
             .threePointArc((s_ * (xb + ri * c45), cyb + ri * c45), (s_ * xb, yc - T / 2))
             .lineTo(s_ * (WIN_XIN - 0.1), yc - T / 2)
             .close()
             .extrude(TAB_Z1 - TAB_Z0))
    strap = strap.edges("|X and <Y").fillet(TAB_TIP_R)
    shell = shell.union(strap)
    # bottom post below the lower window: square-cornered hollow box
    if s_ > 0:
        post = rrect(POST_X0, W / 2, -D / 2, POST_Y1, POST_R_IN, 0.3, 0.3, 0.3)
    else:
        post = rrect(-W / 2, -POST_X0, -D / 2, POST_Y1, 0.3, POST_R_IN, 0.3, 0.3)
    post = post.extrude(LWIN_Z0 + 0.02)
    post = post.faces("<Z").shell(-T)
    shell = shell.union(post)

# ---------------- front wall bottom: opening for the plastic block ----------------
shell = shell.cut(box(-FTAB_X1, FTAB_X1, -D / 2 - 0.1, -D / 2 + T + 0.05, -0.1, FTAB_Z0))
shell = shell.cut(box(-FTAB_X0, FTAB_X0, -D / 2 - 0.1, -D / 2 + T + 0.05, -0.1, FRONT_CUT_Z))

# ---------------- seam (jigsaw joint) on the -Y wall ----------------
# centre line of the butt joint (X, Z) as measured on the front wall
seam_pts = [(0.0, H + 1.0), (0.0, 4.34), (0.18, 4.26), (1.05, 4.47), (1.23, 4.28), (1.23, 3.58),
            (1.05, 3.40), (-1.08, 3.40), (-1.26, 3.22), (-1.26, 2.47), (-1.06, 2.30),
            (-0.20, 2.52), (0.0, 2.40), (0.0, FRONT_CUT_Z - 0.05)]
seam_w = cq.Workplane("XZ").polyline(seam_pts).wire().val()
seam_w = seam_w.fillet(SEAM_R)
seam_o = seam_w.offset2D(SEAM_GAP / 2)[0]
seam_face = cq.Face.makeFromWires(seam_o)
seam_solid = cq.Solid.extrudeLinear(seam_face, cq.Vector(0, -1.2, 0))
seam_solid = cq.Workplane("XY").add(seam_solid).translate((0, -D / 2 + T + 0.05, 0))
shell = shell.cut(seam_solid)

# ---------------- back (+Y) wall latch windows and latches ----------------
for s_ in (1, -1):
    xc = s_ * LATCH_XC
    shell = shell.cut(box(xc - LATCH_W / 2, xc + LATCH_W / 2, D / 2 - T - 0.1, D / 2 + 0.1,
                          LATCH_Z0, LATCH_Z1))
    # latch lip hinged at the top edge of the window, bent outward
    a = math.radians(LATCH_ANG)
    p0 = (D / 2 - T, LATCH_Z1 + 0.02)
    p1 = (D / 2, LATCH_Z1 + 0.02)
    p2 = (D / 2 + LATCH_L * math.sin(a), LATCH_Z1 - LATCH_L * math.cos(a))
    p3 = (p2[0] - T * math.cos(a), p2[1] - T * math.sin(a))
    lat = (cq.Workplane("YZ", origin=(xc, 0, 0))
           .polyline([p0, p1, p2, p3]).close()
           .extrude(LIP_W / 2, both=True))
    shell = shell.union(lat)
    # inner spring hinged at the bottom edge of the window, leaning into the cavity
    b = math.radians(SPR_ANG)
    q0 = (D / 2 - T, LATCH_Z0 - 0.02)
    q1 = (D / 2, LATCH_Z0 - 0.02)
    q2 = (D / 2 - SPR_L * math.sin(b), LATCH_Z0 + SPR_L * math.cos(b))
    q3 = (q2[0] - T * math.cos(b), q2[1] - T * math.sin(b))
    spr = (cq.Workplane("YZ", origin=(xc, 0, 0))
           .polyline([q0, q1, q2, q3]).close()
           .extrude(SPR_W / 2, both=True))
    spr = spr.faces(">Z").edges("not |X").fillet(SPR_W / 2 - 0.02)
    shell = shell.union(spr)
    # notch in the bottom edge of the back wall in front of the bottom post
    shell = shell.cut(box(s_ * BN_X0, s_ * BN_X1, D / 2 - T - 0.1, D / 2 + 0.1, -0.1, BN_Z))
    shell = shell.cut(box(s_ * BS_X0, s_ * BN_X0 + 0.01 * s_, D / 2 - T - 0.1, D / 2 + 0.1, -0.1, BS_Z))
# central bottom notch on the back wall
shell = shell.cut(box(-BM_X, BM_X, D / 2 - T - 0.1, D / 2 + 0.1, -0.1, BM_Z))

# ---------------- feet ----------------
for s in (1, -1):
    foot = box(s * FOOT_X0, s * FOOT_X1, FOOT_Y, 0.0, 0, T)
    foot = foot.edges("|Z and <Y").fillet(0.25)
    # the folded foot reads as a rim with a recessed centre from below
    fp = box(s * (FOOT_X0 + FOOT_RIM), s * (FOOT_X1 - FOOT_RIM), FOOT_Y + FOOT_RIM, -D / 2 + T,
             -0.05, FOOT_POCKET)
    fp = fp.edges("|Z and <Y").fillet(0.25 - FOOT_RIM)
    foot = foot.cut(fp)
    shell = shell.union(foot)

# ---------------- plastic insert ----------------
# inner outline (slightly inside the shell)
ins_prof = [(-W / 2 + T, D / 2 - T), (W / 2 - T, D / 2 - T), (W / 2 - T, -D / 2 + CY),
            (W / 2 - CX, -D / 2 + T), (-W / 2 + CX, -D / 2 + T), (-W / 2 + T, -D / 2 + CY)]
insert = (cq.Workplane("XY").polyline(ins_prof).close().extrude(FLOOR_Z - LWIN_Z1)
          .translate((0, 0, LWIN_Z1)))
# lower part of the insert is square-cornered (seen through the lower side windows)
insert = insert.union(box(-W / 2 + T + 0.02, W / 2 - T - 0.02, -D / 2 + T, D / 2 - T, INS_Z0, LWIN_Z1 + 0.01))
tongue = box(-TONGUE_HW, TONGUE_HW, TONGUE_Y0, TONGUE_Y1, FLOOR_Z - 0.01, TONGUE_TOP)
tongue = tongue.edges("|Z").fillet(0.15)
tongue = tongue.faces(">Z").edges().chamfer(0.08)
insert = insert.union(tongue)
# contacts on the -Y face of the tongue
for i in range(PIN_N):
    x = (i - (PIN_N - 1) / 2) * PIN_P
    cont = box(x - CONT_W / 2, x + CONT_W / 2, TONGUE_Y0 - CONT_PROUD, TONGUE_Y0 + 0.01,
               FLOOR_Z, TONGUE_TOP - 0.2)
    cont = cont.faces(">Z").edges("<Y").fillet(0.1)
    insert = insert.union(cont)

# front plastic block carrying the pins
blk = box(-BLK_HW, BLK_HW, -D / 2 - 0.02, 0.0, 0.0, FRONT_CUT_Z)
blk = blk.faces("<Y").edges(">Z").chamfer(BLK_CH)
insert = insert.union(blk)
for i in range(PIN_N):
    x = (i - (PIN_N - 1) / 2) * PIN_P
    pin = box(x - PIN_W / 2, x + PIN_W / 2, -D / 2 - 0.02 - PIN_PROUD, -D / 2, 0.0, PIN_H)
    pin = pin.faces(">Z").edges("<Y").fillet(0.09)
    insert = insert.union(pin)

result = shell.union(insert)
